import math
import cadquery as cq

# ============================================================
# Bracket: flanged back plate (XZ plane) with two trapezoidal
# gussets reaching toward -Y, a common cross bore, bosses,
# small triangular ribs, zip-tie style slots and bolt holes.
# ============================================================

# ---------------- driving dimensions (mm) ----------------
PW = 167.5        # plate width (X)
PH = 237.0        # plate height incl. tabs (Z)
PT = 20.0         # plate thickness (Y); plate occupies Y in [0, PT]
NOTCH = 19.4      # corner notch size (X and Z), S-shaped
NR = NOTCH / 2.0  # radius of the three arcs forming each S-notch
TAB_W = PW - 2 * NOTCH   # width of the top / bottom tabs

G_IN = 44.5       # gusset inner face |X|
G_T = 20.0        # gusset thickness (X)
G_DEPTH = 140.0   # gusset reach in -Y from plate front face
G_NOSE = 30.0     # half height of the gusset nose
G_ROOT = PH / 2 - NOTCH   # half height of gusset at the plate

SLOT_W = 26.9     # central plate slot width (X)
SLOT_X = -1.8     # slot centre offset (X)
SLOT_H = 2 * G_ROOT
SLOT_R = 1.0

HOLE_D = 9.0      # plate bolt holes
EDGE = 10.0       # hole distance from plate edge
TOP_HOLES_X = [-44.4, -14.75, 14.75, 44.4]
SIDE_HOLES_Z = [-65.25, -21.75, 21.75, 65.25]

RIB_X = 19.5      # rib leg along the plate (X)
RIB_Y = 38.0      # rib leg along the gusset (Y)
RIB_T = 19.5      # rib thickness (Z)
RIB_Z0 = 29.75    # rib lower face height

AX_Y = -98.75     # main cross bore axis (Y), at Z = 0
BORE_D = 37.7
CB_D = 44.8       # counterbore diameter (opens toward +X on both gussets)
CB_DEPTH_R = 16.0 # right gusset, from its outer face
CB_DEPTH_L = 15.5 # left gusset, from its inner face
TIP_K = 1.09      # teardrop tip distance / radius (tip points to -Y)
CH = 1.5          # 45 deg chamfer on bore ends

BOSS_D0 = 55.5    # conical boss base diameter
BOSS_D1 = 43.5    # conical boss top diameter
BOSS_H_R = 6.5    # right gusset boss height (inner side, -X)
BOSS_H_L = 8.3    # left gusset boss height (outer side, -X)

SM_Y = -51.7      # small bore on left gusset
SM_D = 19.5
SM_CB_D = 38.5
SM_CB_DEPTH = 15.0
SM_BOSS_D = 36.3
SM_BOSS_H = 2.1

SL_Y0, SL_Y1 = -72.9, -32.0   # blind slots in the right gusset outer face (Y extent)
SL_W = 8.3
SL_BULGE = 1.0    # the -Y end of each slot is a shallow arc
SL_DEPTH = 17.0
SL_Z = [-43.45, -17.55, 17.55, 43.45]


# ---------------- helpers ----------------
SEAM_ANG = math.radians(135.0)   # circle seam direction in the YZ plane (from +Y toward +Z)
_SY, _SZ = math.cos(SEAM_ANG), math.sin(SEAM_ANG)


def x_plane(x0):
    """Plane normal to +X at x=x0 whose local x axis points along the seam direction."""
    return cq.Plane(origin=(x0, 0, 0), xDir=(0, _SY, _SZ), normal=(1, 0, 0))


def yz(y, z):
    """(Y, Z) world -> local coords of x_plane (local y = normal x xDir)."""
    # local x = ( _SY, _SZ), local y = (-_SZ, _SY) expressed in (Y, Z)
    return (y * _SY + z * _SZ, -y * _SZ + z * _SY)


def yz_dir(dy, dz):
    return yz(dy, dz)


def x_cylinder(x0, length, y, z, d):
    return cq.Workplane(x_plane(x0)).center(*yz(y, z)).circle(d / 2.0).extrude(length)


def x_teardrop(x0, length, y, z, d, k=TIP_K):
    """Prism along +X with teardrop section: circle plus a point toward -Y."""
    r = d / 2.0
    t = k * r
    phi = math.acos(r / t)
    cx, cy = yz(y, z)
    ux, uy = yz_dir(-1.0, 0.0)   # unit vector toward -Y in local coords
    vx, vy = -uy, ux             # perpendicular
    cp, sp = math.cos(phi), math.sin(phi)
    p1 = (cx + r * (cp * ux + sp * vx), cy + r * (cp * uy + sp * vy))
    p2 = (cx + r * (cp * ux - sp * vx), cy + r * (cp * uy - sp * vy))
    far = (cx - r * ux, cy - r * uy)
    tip = (cx + t * ux, cy + t * uy)
    return (cq.Workplane(x_plane(x0)).moveTo(*p1)
            .threePointArc(far, p2).lineTo(*tip).close().extrude(length))


# ---------------- plate outline with S-shaped corner notches ----------------
def corner_path(sx, sz, reverse):
    a, h, R = TAB_W / 2.0, PH / 2.0, NR
    s = math.sqrt(0.5)
    c1, c2, c3 = (a - R, h - R), (a + R, h - R), (a + R, h - 3 * R)
    start = (a - R, h)
    arcs = [((c1[0] + R * s, c1[1] + R * s), (a, h - R)),          # convex
            ((c2[0] - R * s, c2[1] - R * s), (a + R, h - 2 * R)),  # concave
            ((c3[0] + R * s, c3[1] + R * s), (a + 2 * R, h - 3 * R))]  # convex
    f = lambda p: (sx * p[0], sz * p[1])
    start = f(start)
    arcs = [(f(m), f(e)) for m, e in arcs]
    if reverse:
        ends = [start] + [e for _, e in arcs]
        mids = [m for m, _ in arcs]
        start = ends[-1]
        arcs = [(mids[i], ends[i]) for i in range(len(arcs) - 1, -1, -1)]
    return start, arcs


wp = cq.Workplane("XZ")
first = True
for sx, sz, rev in ((1, 1, False), (1, -1, True), (-1, -1, False), (-1, 1, True)):
    st, arcs = corner_path(sx, sz, rev)
    wp = wp.moveTo(*st) if first else wp.lineTo(*st)
    first = False
    for m, e in arcs:
        wp = wp.threePointArc(m, e)
plate = wp.close().extrude(-PT)          # XZ normal is -Y -> plate spans Y 0..PT

# ---------------- gussets ----------------
g_pts = [(0, G_ROOT), (-G_DEPTH, G_NOSE), (-G_DEPTH, -G_NOSE), (0, -G_ROOT)]
g_right = cq.Workplane("YZ", origin=(G_IN, 0, 0)).polyline(g_pts).close().extrude(G_T)
g_left = cq.Workplane("YZ", origin=(-G_IN - G_T, 0, 0)).polyline(g_pts).close().extrude(G_T)

body = plate.union(g_right).union(g_left)


# ---------------- triangular ribs (gusset inner face to plate) ----------------
def rib(side, z0):
    x0 = side * G_IN
    pts = [(x0, 0), (x0 - side * RIB_X, 0), (x0, -RIB_Y)]
    return cq.Workplane("XY", origin=(0, 0, z0)).polyline(pts).close().extrude(RIB_T)


for s in (-1, 1):
    for z0 in (RIB_Z0, -RIB_Z0 - RIB_T):
        body = body.union(rib(s, z0))


# ---------------- bosses (all on the -X side of their gusset) ----------------
def cone_boss(x_face, h, d0, d1, y, z):
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(d0 / 2.0, d1 / 2.0, h,
                          pnt=cq.Vector(x_face, y, z),
                          dir=cq.Vector(-1, 0, 0)))


body = body.union(cone_boss(G_IN, BOSS_H_R, BOSS_D0, BOSS_D1, AX_Y, 0))
body = body.union(cone_boss(-G_IN - G_T, BOSS_H_L, BOSS_D0, BOSS_D1, AX_Y, 0))
body = body.union(x_cylinder(-G_IN - G_T - SM_BOSS_H, SM_BOSS_H + 0.5, SM_Y, 0, SM_BOSS_D))

# ---------------- plate slot and bolt holes ----------------
slot_sk = cq.Sketch().rect(SLOT_W, SLOT_H).vertices().fillet(SLOT_R)
slot = (cq.Workplane("XZ", origin=(0, PT + 1, 0)).center(SLOT_X, 0)
        .placeSketch(slot_sk).extrude(PT + 2))
body = body.cut(slot)

hole_pts = [(x, z) for x in TOP_HOLES_X for z in (PH / 2 - EDGE, -PH / 2 + EDGE)]
hole_pts += [(x, z) for x in (PW / 2 - EDGE, -PW / 2 + EDGE) for z in SIDE_HOLES_Z]
holes = (cq.Workplane("XZ", origin=(0, PT + 1, 0)).pushPoints(hole_pts)
         .circle(HOLE_D / 2).extrude(PT + 2))
body = body.cut(holes)

# ---------------- cross bore, counterbores, small bore ----------------
X_MIN = -G_IN - G_T - BOSS_H_L - 2
X_MAX = G_IN + G_T + 2
body = body.cut(x_cylinder(X_MIN, X_MAX - X_MIN, AX_Y, 0, BORE_D))
body = body.cut(x_teardrop(G_IN + G_T - CB_DEPTH_R, CB_DEPTH_R + 1, AX_Y, 0, CB_D))
body = body.cut(x_teardrop(-G_IN - CB_DEPTH_L, CB_DEPTH_L + 1, AX_Y, 0, CB_D))

body = body.cut(x_cylinder(X_MIN, 30, SM_Y, 0, SM_D))
body = body.cut(x_cylinder(-G_IN - SM_CB_DEPTH, SM_CB_DEPTH + 1, SM_Y, 0, SM_CB_D))


def bore_chamfer(x_face, outward, y, d, c=CH):
    """45 deg conical countersink at a bore mouth lying in plane x = x_face;
    outward = +1/-1 is the direction pointing out of the material."""
    e = 0.2
    r0 = d / 2.0 + c + e
    length = c + e + 0.5
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(r0, r0 - length, length,
                          pnt=cq.Vector(x_face + outward * e, y, 0),
                          dir=cq.Vector(-outward, 0, 0)))


# chamfers: big bore at both boss tops, small bore at both ends
body = body.cut(bore_chamfer(-G_IN - G_T - BOSS_H_L, -1, AX_Y, BORE_D))
body = body.cut(bore_chamfer(G_IN - BOSS_H_R, -1, AX_Y, BORE_D))
body = body.cut(bore_chamfer(-G_IN - G_T - SM_BOSS_H, -1, SM_Y, SM_D))
body = body.cut(bore_chamfer(-G_IN - SM_CB_DEPTH, +1, SM_Y, SM_D))

# ---------------- blind slots in right gusset outer face ----------------
def gusset_slot(z):
    """Blind slot: square +Y end, shallow arc at the -Y end."""
    y0 = SL_Y0 + SL_BULGE          # arc end points
    y1, zt, zb = SL_Y1, z + SL_W / 2, z - SL_W / 2
    return (cq.Workplane("YZ", origin=(G_IN + G_T - SL_DEPTH, 0, 0))
            .moveTo(y0, zt).lineTo(y1, zt).lineTo(y1, zb).lineTo(y0, zb)
            .threePointArc((SL_Y0, z), (y0, zt))
            .close()
            .extrude(SL_DEPTH + 1))


for z in SL_Z:
    body = body.cut(gusset_slot(z))

result = body
